"""Open-backed electronics enclosure: display window + two round holes in the
front wall, standoff pins on the inside of the front wall and locating pins on
the open back rim."""
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 64.0        # overall width  (X)
H = 100.0       # overall height (Z)
D = 43.0        # overall depth  (Y), front face at -Y, open back at +Y
T_FRONT = 4.5   # front wall
T_SIDE = 6.0    # left / right walls
T_TOP = 6.0     # top wall
T_BOT = 3.0     # bottom wall

# display window in the front wall
WIN_W = 39.0
WIN_H = 52.8
WIN_TOP = 12.2          # margin from top edge to window

# two round holes
HOLE_D = 19.0
HOLE_DX = 14.0          # +/- from centre
HOLE_Z = 14.9           # from bottom edge

# locating pins on the back rim (4 corners)
RIM_PIN_D = 4.2
RIM_PIN_L = 3.3
RIM_PIN_SHORT_L = 2.8   # the lower pin on the -X side is a short stub
RIM_PIN_SHORT_Z = 2.7
RIM_PIN_CHAMFER = 0.5   # chamfer on the pin tips
RIM_PIN_IN_X = 3.0      # pin axis from side faces
RIM_PIN_IN_Z = 3.3      # pin axis from top / bottom faces
KEY_HOLE_D = 3.6        # small blind hole in the -X rim above the stub
KEY_HOLE_DEPTH = 1.0
KEY_HOLE_Z = 7.6

# display standoff pins (inner face of front wall, pointing +Y)
DPIN_D = 2.6
DPIN_L = 13.6
DPIN_DX = 16.2          # +/- from centre
DPIN_DZ = 29.0          # +/- from window centre

# pins beside the round holes
HPIN_D = 2.6
HPIN_L = 10.6
HPIN_DX = 9.0           # outboard of hole centre
HPIN_DZ = 9.75          # +/- from hole centre

# ---------------- body ----------------
outer = cq.Workplane("XY").box(W, D, H, centered=(True, True, False))
cavity = (cq.Workplane("XY")
          .box(W - 2 * T_SIDE, D - T_FRONT + 1.0, H - T_TOP - T_BOT,
               centered=(True, False, False))
          .translate((0, -D / 2 + T_FRONT, T_BOT)))
body = outer.cut(cavity)

# window
win_zc = H - WIN_TOP - WIN_H / 2
window = (cq.Workplane("XZ").center(0, win_zc)
          .rect(WIN_W, WIN_H).extrude(-(T_FRONT + 2)).translate((0, -D / 2 - 1, 0)))
body = body.cut(window)

# round holes
holes = (cq.Workplane("XZ").pushPoints([(-HOLE_DX, HOLE_Z), (HOLE_DX, HOLE_Z)])
         .circle(HOLE_D / 2).extrude(-(T_FRONT + 2)).translate((0, -D / 2 - 1, 0)))
body = body.cut(holes)

# ---------------- pins ----------------
SEAM_TURN = 120.0   # turn each pin about its own axis so its seam line faces -X/-Z


def pin_y(x, z, y0, length, dia, chamfer=0.0):
    """Cylindrical pin with axis parallel to +Y, starting at y0."""
    p = (cq.Workplane("XZ", origin=(0, y0, 0)).center(x, z)
         .circle(dia / 2).extrude(-length))
    if chamfer > 0:
        p = p.faces(">Y").edges().chamfer(chamfer)
    return p.rotate((x, 0, z), (x, 1, z), SEAM_TURN)


# rim pins on the open back face (chamfered tips)
px = W / 2 - RIM_PIN_IN_X
for (x, z, length) in [(px, RIM_PIN_IN_Z, RIM_PIN_L),
                       (px, H - RIM_PIN_IN_Z, RIM_PIN_L),
                       (-px, H - RIM_PIN_IN_Z, RIM_PIN_L),
                       (-px, RIM_PIN_SHORT_Z, RIM_PIN_SHORT_L)]:
    body = body.union(pin_y(x, z, D / 2, length, RIM_PIN_D, RIM_PIN_CHAMFER))

# small blind hole in the -X rim
key_hole = (cq.Workplane("XZ", origin=(0, D / 2, 0)).center(-px, KEY_HOLE_Z)
            .circle(KEY_HOLE_D / 2).extrude(KEY_HOLE_DEPTH))
body = body.cut(key_hole)

# internal pins on the inner face of the front wall
inner_y = -D / 2 + T_FRONT
for sx in (-1, 1):
    for sz in (-1, 1):
        # display standoffs around the window
        body = body.union(pin_y(sx * DPIN_DX, win_zc + sz * DPIN_DZ,
                                inner_y, DPIN_L, DPIN_D))
        # pins outboard of the round holes
        body = body.union(pin_y(sx * (HOLE_DX + HPIN_DX), HOLE_Z + sz * HPIN_DZ,
                                inner_y, HPIN_L, HPIN_D))

result = body
